import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0            # octagon flat-to-flat width
H = 13.8             # overall height (wall height)
T_WALL = 3.6         # wall thickness
OCT_ROT = 1.2        # octagon frame is turned slightly (deg, CCW seen from top)
Z_FB = 0.4           # floor underside (slightly recessed from wall bottom)
Z_FT = 6.95          # floor top

# windows in every wall flat (two per flat)
WIN_W = 14.0
PILLAR_W = 4.4
WIN_Z0 = 3.45
WIN_Z1 = 10.35

# radial screw hole through a thin web in the pillar + nut pocket
WALL_HOLE_D = 3.7
WALL_HOLE_Z = 6.9
WEB = 0.5            # web left at the outer face of the pillar
NOTCH_W = 3.5
NOTCH_D = 3.5
POCKET_Z0 = 3.1     # bottom of the nut pocket / pillar recess

# central opening, spokes and hub
R_CENTER = 27.2
SPOKE_W = 4.0
HUB_R = 7.0
HUB_H = H
HUB_BORE_R = 3.7
HUB_TOP_ROUND_H = 3.1     # elliptical shoulder on hub top (radial)
HUB_TOP_ROUND_V = 2.0     # elliptical shoulder on hub top (vertical)
HUB_SPOKE_FILLET = 4.4
HUB_CROSS_D = 2.6
HUB_CROSS_Z = 10.3

# tilted floor holes
N_HOLES = 8
HOLE_D = 14.0
HOLE_TILT = 45.0          # deg from vertical
HOLE_BOT_FILLET = 0.7     # rounded inlet edge on the underside
CENTER_BOT_FILLET = 1.2
HOLE_R = 38.5             # radius of hole centre on the floor top face
HOLE_ANG0 = 21.75
HOLE_DIR_OFFSET = -112.5  # tilt direction relative to hole polar angle
HOLE_TRUNC = 0.7          # tool end cap clips the trailing tip of the outline

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
APO = W / 2.0
R_OUT = APO / math.cos(math.radians(22.5))
APO_IN = APO - T_WALL
R_IN = APO_IN / math.cos(math.radians(22.5))


def octagon_pts(r):
    return [(r * math.cos(math.radians(22.5 + 45 * k)),
             r * math.sin(math.radians(22.5 + 45 * k))) for k in range(8)]


def rotz(wp, ang):
    return wp.rotate((0, 0, 0), (0, 0, 1), ang)


# ---------------- octagonal tray (walls + floor) ----------------
body = cq.Workplane("XY").polyline(octagon_pts(R_OUT)).close().extrude(H)
inner_top = (cq.Workplane("XY").workplane(offset=Z_FT)
             .polyline(octagon_pts(R_IN)).close().extrude(H))
body = body.cut(inner_top)
inner_bot = (cq.Workplane("XY").workplane(offset=-1)
             .polyline(octagon_pts(R_IN)).close().extrude(1 + Z_FB))
body = body.cut(inner_bot)


# wall features, built for the +X flat then patterned around
def flat_cutters():
    cut = None
    for s in (-1, 1):
        yc = s * (PILLAR_W / 2 + WIN_W / 2)
        w = (cq.Workplane("XY")
             .box(T_WALL + 1.0, WIN_W, WIN_Z1 - WIN_Z0)
             .translate((APO_IN + (T_WALL + 1.0) / 2, yc, (WIN_Z0 + WIN_Z1) / 2)))
        cut = w if cut is None else cut.union(w)
    # recess behind the pillar leaving a thin web at the outside
    rec_len = T_WALL - WEB
    rec = (cq.Workplane("XY")
           .box(rec_len + 0.01, PILLAR_W, WIN_Z1 - POCKET_Z0)
           .translate((APO_IN + rec_len / 2 - 0.005, 0, (WIN_Z1 + POCKET_Z0) / 2)))
    cut = cut.union(rec)
    # nut pocket in the floor next to the wall
    pk_h = Z_FT + 1.0 - POCKET_Z0
    notch = (cq.Workplane("XY")
             .box(NOTCH_D + 0.02, NOTCH_W, pk_h)
             .translate((APO_IN - NOTCH_D / 2 + 0.01, 0, POCKET_Z0 + pk_h / 2)))
    cut = cut.union(notch)
    # radial screw hole
    hole = (cq.Workplane("YZ").workplane(offset=APO_IN - 1)
            .center(0, WALL_HOLE_Z).circle(WALL_HOLE_D / 2).extrude(T_WALL + 3))
    cut = cut.union(hole)
    return cut


fc = flat_cutters()
for k in range(8):
    body = body.cut(rotz(fc, 45 * k))

# small pads under the nut pockets (flush with wall bottom)
pad = (cq.Workplane("XY")
       .box(NOTCH_D + 0.02, NOTCH_W, Z_FB + 0.01)
       .translate((APO_IN - NOTCH_D / 2 + 0.01, 0, (Z_FB + 0.01) / 2)))
for k in range(8):
    body = body.union(rotz(pad, 45 * k))

# whole frame sits slightly rotated relative to the spokes / holes
body = rotz(body, OCT_ROT)

# ---------------- central opening ----------------
center_cut = cq.Workplane("XY").workplane(offset=-1).circle(R_CENTER).extrude(H + 2)
body = body.cut(center_cut)

# spokes along X and Y
spoke_len = 2 * R_CENTER + 2.0
spokes = (cq.Workplane("XY").workplane(offset=Z_FB)
          .rect(spoke_len, SPOKE_W).extrude(Z_FT - Z_FB)
          .union(cq.Workplane("XY").workplane(offset=Z_FB)
                 .rect(SPOKE_W, spoke_len).extrude(Z_FT - Z_FB)))
body = body.union(spokes)

# hub with rounded top (seam turned onto the silhouette line)
hub = (cq.Workplane("XZ")
       .moveTo(0, Z_FB)
       .lineTo(HUB_R, Z_FB)
       .lineTo(HUB_R, HUB_H - HUB_TOP_ROUND_V)
       .ellipseArc(HUB_TOP_ROUND_H, HUB_TOP_ROUND_V, 0, 90, startAtCurrent=True)
       .lineTo(0, HUB_H)
       .close()
       .revolve(360, (0, 0, 0), (0, 1, 0)))
hub = rotz(hub, 45)
body = body.union(hub)

# concave fillets between spoke tops and hub: torus ring clipped to spokes
rf = HUB_SPOKE_FILLET
ring = (cq.Workplane("XZ")
        .moveTo(HUB_R - 0.3, Z_FT - 0.01)
        .lineTo(HUB_R + rf, Z_FT - 0.01)
        .lineTo(HUB_R + rf, Z_FT)
        .radiusArc((HUB_R, Z_FT + rf), rf)
        .lineTo(HUB_R - 0.3, Z_FT + rf)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
ring = rotz(ring, 45)
slab_len = 2 * (HUB_R + rf + 1)
slabs = (cq.Workplane("XY").workplane(offset=Z_FT - 0.5)
         .rect(slab_len, SPOKE_W).extrude(rf + 1)
         .union(cq.Workplane("XY").workplane(offset=Z_FT - 0.5)
                .rect(SPOKE_W, slab_len).extrude(rf + 1)))
body = body.union(ring.intersect(slabs))

# hub bore and cross hole (along Y)
bore = cq.Workplane("XY").workplane(offset=-1).circle(HUB_BORE_R).extrude(H + 2)
body = body.cut(bore)
cross = (cq.Workplane("XZ").workplane(offset=-30)
         .center(0, HUB_CROSS_Z).circle(HUB_CROSS_D / 2).extrude(60))
body = body.cut(cross)

# ---------------- tilted floor holes ----------------
alpha = math.radians(HOLE_TILT)
for k in range(N_HOLES):
    th = math.radians(HOLE_ANG0 + 45 * k)
    tdir = th + math.radians(HOLE_DIR_OFFSET)
    tx, ty = math.cos(tdir), math.sin(tdir)
    p_top = cq.Vector(HOLE_R * math.cos(th), HOLE_R * math.sin(th), Z_FT)
    up = cq.Vector(-math.sin(alpha) * tx, -math.sin(alpha) * ty, math.cos(alpha))
    # seam of the cylinder placed on the flank that faces away from the
    # default camera (flank generators are hidden under top/bottom faces)
    nx, ny = -ty, tx
    if (nx - ny) < 0:
        nx, ny = -nx, -ny
    xd = cq.Vector(nx, ny, 0.0)
    pl = cq.Plane(origin=p_top, xDir=xd, normal=up)
    # tool starts just above the floor top (so it never reaches the walls)
    # (end cap slightly clips the trailing tip of the top outline)
    cap = (HOLE_D / 2.0) * math.tan(alpha) - HOLE_TRUNC * math.sin(alpha)
    cyl = (cq.Workplane(pl).workplane(offset=cap)
           .circle(HOLE_D / 2.0).extrude(-(cap + 20.0)))
    body = body.cut(cyl)

# rounded underside edges of the tilted holes and the central opening
def _bottom_edges(shape, rmin, rmax):
    out = []
    for e in shape.edges().vals():
        bb = e.BoundingBox()
        if abs(bb.zmin - Z_FB) < 1e-3 and abs(bb.zmax - Z_FB) < 1e-3:
            c = e.Center()
            r = math.hypot(c.x, c.y)
            if rmin < r < rmax:
                out.append(e)
    return out


hole_edges = [e for e in _bottom_edges(body, 30.0, 47.0)
              if e.geomType() in ("ELLIPSE", "BSPLINE", "CIRCLE")]
body = body.newObject(hole_edges).fillet(HOLE_BOT_FILLET)
ctr_edges = [e for e in _bottom_edges(body, 15.0, 30.0)
             if e.geomType() == "CIRCLE"]
body = body.newObject(ctr_edges).fillet(CENTER_BOT_FILLET)

result = body
